import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 100.0          # overall width (X) and depth (Y) - square housing
H = 21.0           # body height from rim to top face
R_PLAN = 12.5      # plan corner radius
C_TOP = 4.1        # 45 deg chamfer around the top
T_WALL = 2.2       # side wall thickness (also across the top chamfer)
T_TOP = 2.6        # top plate thickness
R_INNER = 11.6     # plan corner radius of the cavity (corners slightly thicker)

# feet / screw bosses (protrude below the rim)
BOSS_D = 6.8
BOSS_HOLE = 2.4
FOOT_H = 5.3
FRONT_BOSS_X = 44.4
FRONT_BOSS_Y = -33.0
BACK_BOSS_X = 33.5
BACK_BOSS_Y = 44.3

# internal PCB standoffs (hang from the top plate)
STANDOFF_X = -38.0
STANDOFF_YS = (4.3, 32.6)
STANDOFF_Z = 10.6          # bottom face height

# internal stiffening rib along X
RIB_Y = -1.45
RIB_T = 1.5
RIB_X0 = -35.1
RIB_Z = 12.2               # bottom edge height

# half-round guide ribs on the inside of the right wall
GUIDE_YS = (-5.7, 21.9)
GUIDE_R = 2.6
GUIDE_Z0 = 0.0

# vents on the back edge
VENT_N = 4
VENT_W = 2.3
VENT_PITCH = 4.7
VENT_X0 = -28.7            # x of first vent centre
VENT_Y_END = 23.5          # inner end of vent on top face
VENT_Z_END = 6.0           # lower end of vent on back wall
VENT_BAR_Y = (43.1, 45.0)  # small bridging bar under the vents
VENT_BAR_DEPTH = 2.6

# LED holes
LED_D = 2.6
LED_X = 22.6
LED_YS = (34.85, 22.9, 14.8)

# front wall slots
FSLOT_X = 34.4
FSLOT_Z = 9.8
FSLOT_W = 2.7
FSLOT_H = 6.6

# ---------------- shell ----------------
def rounded_square_wire(side, r, z, seam_x):
    """Rounded-square outline (lines + tangent arcs) merged into ONE exact B-spline edge,
    so the side wall becomes a single smooth face. The seam starts at (seam_x, +side/2)."""
    hw = side / 2.0
    s = math.sqrt(0.5)
    V = lambda x, y: cq.Vector(x, y, z)
    edges = [
        cq.Edge.makeLine(V(seam_x, hw), V(hw - r, hw)),
        cq.Edge.makeThreePointArc(V(hw - r, hw), V(hw - r + r * s, hw - r + r * s), V(hw, hw - r)),
        cq.Edge.makeLine(V(hw, hw - r), V(hw, -hw + r)),
        cq.Edge.makeThreePointArc(V(hw, -hw + r), V(hw - r + r * s, -hw + r - r * s), V(hw - r, -hw)),
        cq.Edge.makeLine(V(hw - r, -hw), V(-hw + r, -hw)),
        cq.Edge.makeThreePointArc(V(-hw + r, -hw), V(-hw + r - r * s, -hw + r - r * s), V(-hw, -hw + r)),
        cq.Edge.makeLine(V(-hw, -hw + r), V(-hw, hw - r)),
        cq.Edge.makeThreePointArc(V(-hw, hw - r), V(-hw + r - r * s, hw - r + r * s), V(-hw + r, hw)),
        cq.Edge.makeLine(V(-hw + r, hw), V(seam_x, hw)),
    ]
    try:
        from OCP.BRep import BRep_Tool
        from OCP.Geom import Geom_TrimmedCurve
        from OCP.GeomConvert import GeomConvert, GeomConvert_CompCurveToBSplineCurve
        from OCP.BRepBuilderAPI import BRepBuilderAPI_MakeEdge, BRepBuilderAPI_MakeWire

        conv = None
        for e in edges:
            f, l = e._bounds()
            bs = GeomConvert.CurveToBSplineCurve_s(Geom_TrimmedCurve(BRep_Tool.Curve_s(e.wrapped, f, l), f, l))
            if conv is None:
                conv = GeomConvert_CompCurveToBSplineCurve(bs)
            elif not conv.Add(bs, 1e-7, True):
                raise RuntimeError("curve join failed")
        edge = BRepBuilderAPI_MakeEdge(conv.BSplineCurve()).Edge()
        return cq.Wire(BRepBuilderAPI_MakeWire(edge).Wire())
    except Exception:
        return cq.Wire.assembleEdges(edges)


def rounded_prism(side, r, z0, height, chamfer, seam_x):
    """Rounded-square prism with a 45 deg chamfer round the top: the wall is a linear
    extrusion of one smooth outline, the chamfer a ruled loft - one face each."""
    zc = z0 + height - chamfer
    base = rounded_square_wire(side, r, z0, seam_x)
    wall = cq.Solid.extrudeLinear(cq.Face.makeFromWires(base), cq.Vector(0, 0, zc - z0))
    cham = cq.Solid.makeLoft(
        [rounded_square_wire(side, r, zc, seam_x),
         rounded_square_wire(side - 2 * chamfer, r - chamfer, z0 + height, seam_x)],
        True,
    )
    return cq.Workplane("XY").add(wall).union(cq.Workplane("XY").add(cham), clean=False)


SEAM_X = VENT_X0 + VENT_PITCH     # seam of the smooth side faces, hidden inside a vent slot
outer = rounded_prism(W, R_PLAN, 0.0, H, C_TOP, SEAM_X)
# inner cavity: the outer form offset inward by the wall thickness (open at the bottom)
C_IN = C_TOP + T_WALL * (math.sqrt(2.0) - 1.0) - T_TOP   # keeps the chamfer zone T_WALL thick
void = rounded_prism(W - 2 * T_WALL, R_INNER, -1.0, H - T_TOP + 1.0, C_IN, SEAM_X)
# same cavity built with ordinary fillets: used only to trim the internal features
void_trim = (
    cq.Workplane("XY").workplane(offset=-1.0)
    .rect(W - 2 * T_WALL, W - 2 * T_WALL)
    .extrude(H - T_TOP + 1.0)
    .edges("|Z").fillet(R_INNER)
    .faces(">Z").edges().chamfer(C_IN)
)
body = outer.cut(void, clean=False)

inner_half = W / 2 - T_WALL
PLATE_Z = H - T_TOP


def web_boss(x, y, toward):
    """Cylinder boss joined to the nearest wall by a web, protruding below the rim."""
    h = H + FOOT_H
    base = cq.Workplane("XY").workplane(offset=-FOOT_H)
    cyl = base.center(x, y).circle(BOSS_D / 2).extrude(h)
    if toward == "+x":
        L = inner_half - x + 1.0
        web = base.center(x + L / 2, y).rect(L, BOSS_D).extrude(h)
    elif toward == "-x":
        L = x + inner_half + 1.0
        web = base.center(x - L / 2, y).rect(L, BOSS_D).extrude(h)
    else:  # +y
        L = inner_half - y + 1.0
        web = base.center(x, y + L / 2).rect(BOSS_D, L).extrude(h)
    return cyl.union(web)


# everything that hangs inside the shell is trimmed to the cavity (plus the region below the rim)
keep = void_trim.union(
    cq.Workplane("XY").workplane(offset=-FOOT_H - 1).rect(W - 2 * T_WALL, W - 2 * T_WALL).extrude(FOOT_H + 1)
)

feet = [
    (-FRONT_BOSS_X, FRONT_BOSS_Y, "-x"),
    (FRONT_BOSS_X, FRONT_BOSS_Y, "+x"),
    (-BACK_BOSS_X, BACK_BOSS_Y, "+y"),
    (BACK_BOSS_X, BACK_BOSS_Y, "+y"),
]
inner = None
for (x, y, t) in feet:
    b = web_boss(x, y, t)
    inner = b if inner is None else inner.union(b)

# PCB standoffs
for y in STANDOFF_YS:
    s = (
        cq.Workplane("XY").workplane(offset=STANDOFF_Z)
        .center(STANDOFF_X, y).circle(BOSS_D / 2).extrude(H - STANDOFF_Z)
    )
    inner = inner.union(s)

# rib along X from the left standoff region to the right wall
rib_len = inner_half + 1.0 - RIB_X0
rib = (
    cq.Workplane("XY").workplane(offset=RIB_Z)
    .center(RIB_X0 + rib_len / 2, RIB_Y).rect(rib_len, RIB_T).extrude(H - RIB_Z)
)
inner = inner.union(rib)

# half-round locating ribs on the inside of the right wall
for y in GUIDE_YS:
    g = (
        cq.Workplane("XY").workplane(offset=GUIDE_Z0)
        .center(inner_half, y).circle(GUIDE_R).extrude(H - GUIDE_Z0)
    )
    inner = inner.union(g)

inner = inner.intersect(keep)
body = body.union(inner, clean=False)

# screw holes (blind, from below)
foot_pts = [(x, y) for (x, y, _) in feet]
holes = (
    cq.Workplane("XY").workplane(offset=-FOOT_H - 1)
    .pushPoints(foot_pts).circle(BOSS_HOLE / 2).extrude(FOOT_H + PLATE_Z - 1.0)
)
body = body.cut(holes, clean=False)
sholes = (
    cq.Workplane("XY").workplane(offset=STANDOFF_Z - 1)
    .pushPoints([(STANDOFF_X, y) for y in STANDOFF_YS]).circle(BOSS_HOLE / 2)
    .extrude(PLATE_Z - STANDOFF_Z)
)
body = body.cut(sholes, clean=False)

# ---------------- vents ----------------
vent_xs = [VENT_X0 + i * VENT_PITCH for i in range(VENT_N)]
vent_cutter = None
for x in vent_xs:
    L = W / 2 + 2 - VENT_Y_END
    top_cut = (
        cq.Workplane("XY").workplane(offset=H - C_TOP - T_WALL - 1.0)
        .center(x, VENT_Y_END + L / 2)
        .slot2D(L, VENT_W, angle=90)
        .extrude(C_TOP + T_WALL + 3)
    )
    Lz = H + 2 - VENT_Z_END
    wall_cut = (
        cq.Workplane("XZ", origin=(0, W / 2 + 1, 0))
        .center(x, VENT_Z_END + Lz / 2)
        .slot2D(Lz, VENT_W, angle=90)
        .extrude(T_WALL + C_TOP + 2)
    )
    cutter = top_cut.union(wall_cut)          # one cutter -> one face per slot side
    vent_cutter = cutter if vent_cutter is None else vent_cutter.union(cutter)
body = body.cut(vent_cutter, clean=False)

# small bar bridging the vents on the inside, near the back wall
bar_len = (vent_xs[-1] - vent_xs[0]) + VENT_W + 2.0
bar = (
    cq.Workplane("XY").workplane(offset=PLATE_Z - VENT_BAR_DEPTH)
    .center((vent_xs[0] + vent_xs[-1]) / 2, (VENT_BAR_Y[0] + VENT_BAR_Y[1]) / 2)
    .rect(bar_len, VENT_BAR_Y[1] - VENT_BAR_Y[0])
    .extrude(VENT_BAR_DEPTH + 0.5)
)
body = body.union(bar, clean=False)

# ---------------- LED holes ----------------
leds = (
    cq.Workplane("XY").workplane(offset=PLATE_Z - 1)
    .pushPoints([(LED_X, y) for y in LED_YS]).circle(LED_D / 2).extrude(T_TOP + 2)
)
body = body.cut(leds, clean=False)

# ---------------- front wall slots ----------------
fslots = (
    cq.Workplane("XZ", origin=(0, -W / 2 - 1, 0))
    .pushPoints([(-FSLOT_X, FSLOT_Z), (FSLOT_X, FSLOT_Z)])
    .slot2D(FSLOT_H, FSLOT_W, angle=90)
    .extrude(-(T_WALL + 2))
)
body = body.cut(fslots, clean=False)

result = body
